import cadquery as cq
import math

# =====================================================================
#  Small electronics enclosure with sliding-lid grooves
#  (box open on top, lid slides in from the back over the lowered
#   back wall; USB-style port in the front, side port + slot, wall-
#   mount keyholes, PCB posts, connector cradle and module clip)
# =====================================================================

# ---------------- overall dimensions (mm) ----------------
W = 100.0        # outer width  (X)
D = 100.0        # outer depth  (Y)
H = 29.2         # outer height (Z)
T = 2.85         # wall thickness
F = 2.8          # floor thickness

# sliding-lid groove (on -X, +X and -Y walls; back wall lowered)
G_FLOOR = 25.4   # groove floor height (= back wall top)
G_CEIL = 28.0    # groove ceiling height
G_DEPTH = 1.35   # groove depth into the wall

# front (-Y) port, near the +X end
FP_X0, FP_X1 = 29.3, 40.5
FP_Z0, FP_Z1 = 4.65, 13.2
FP_R_BOT = 0.6   # also the channel's bottom fillet
FP_R_TOP = 0.4

# right (+X) side obround slot
SS_Y, SS_Z = -43.2, 9.1
SS_L, SS_H = 4.6, 2.8

# left (-X) side port
LP_Y, LP_Z = -24.0, 7.1
LP_W, LP_H = 9.0, 8.0
LP_R = 0.4

# blind round recess on the inside of the -X wall
LR_Y, LR_Z, LR_D, LR_DEPTH = -27.9, 16.8, 6.0, 1.0

# keyholes in the floor
KH_X = 23.5
KH_Y = 28.35
KH_R = 3.75       # big circle radius
KH_SLOT_W = 3.95  # slot width
KH_SLOT_L = 5.75  # big-circle centre to slot-end centre (towards +Y)

# D-shaped PCB posts (cross pattern around the centre)
POST_H = 2.9
P_IN_C, P_IN_R, P_IN_FLAT = 11.4, 2.1, 12.4    # flat faces outward
P_OUT_C, P_OUT_R, P_OUT_FLAT = 19.0, 2.0, 18.2  # flat faces inward

# module clip near the front-left corner
SP_X0, SP_X1 = -36.8, -35.2       # spine
SP_Y0, SP_Y1 = -42.5, -19.6
SP_TOP = 21.0
GUS_Y = (-20.1, -31.1, -41.9)     # gusset centres
GUS_T = 1.0
GUS_TOP_X = -34.7
GUS_BOT_X = -31.6
TAB_X1 = -41.5                    # wall tabs reach
TAB_Y = (-19.3, -17.1)
CB_Y = -44.1                      # corner block inner face

# connector cradle in the front-right corner
CR_X0 = 21.4
CR_Y0, CR_Y1 = -D / 2 + T, -4.9
CR_TOP = 8.2          # back strip top
CR_BASE_Z = 6.6       # front rim / side rim top
CR_RIM = 1.2
CR_POCKET_Y0 = -40.5  # back face of the front rim
CR_STRIP_Y0 = -18.6   # front face of the back strip
CR_LEDGE_Y1 = -14.3   # back end of the ledge
CR_LEDGE_Z = 6.2      # ledge height
CR_HOLE = (34.9, -9.8, 3.0)


# ---------------- helpers ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


XI = W / 2 - T   # inner half width
YI = D / 2 - T   # inner half depth

# ---------------- shell ----------------
body = box(-W / 2, W / 2, -D / 2, D / 2, 0, H)
body = body.cut(box(-XI, XI, -YI, YI, F, H + 1))

# ---------------- interior features (added before the cuts) ----------------
# D-posts: 4 pairs on the +/-X and +/-Y axes
def d_post(cx, cy, r, keep_dir, flat_off):
    """cylinder radius r at (cx,cy) cut by a flat; keep_dir is a unit axis
    vector (dx,dy) pointing towards the kept side of the flat."""
    cyl = (cq.Workplane("XY").circle(r).extrude(POST_H)
           .translate((cx, cy, F)))
    dx, dy = keep_dir
    # the material beyond the flat (opposite to keep_dir) is removed
    big = 4 * r
    fx = cx - dx * flat_off
    fy = cy - dy * flat_off
    cutter = (cq.Workplane("XY").box(big, big, POST_H * 3)
              .translate((fx - dx * big / 2, fy - dy * big / 2, F + POST_H / 2)))
    return cyl.cut(cutter)


posts = None
for ax, ay in ((1, 0), (-1, 0), (0, 1), (0, -1)):
    # inner post: flat on the outward side, keep the part towards centre
    pin = d_post(ax * P_IN_C, ay * P_IN_C, P_IN_R, (-ax, -ay),
                 (P_IN_FLAT - P_IN_C))
    # outer post: flat on the inward side, keep the part away from centre
    pout = d_post(ax * P_OUT_C, ay * P_OUT_C, P_OUT_R, (ax, ay),
                  (P_OUT_C - P_OUT_FLAT))
    for p in (pin, pout):
        posts = p if posts is None else posts.union(p)
body = body.union(posts)

# module clip: spine wall + three triangular gussets
spine = box(SP_X0, SP_X1, SP_Y0, SP_Y1, F - 0.01, SP_TOP)
body = body.union(spine)
for gy in GUS_Y:
    gus = (cq.Workplane("XZ")
           .polyline([(SP_X1 - 0.01, F - 0.01), (GUS_BOT_X, F - 0.01),
                      (GUS_TOP_X, SP_TOP), (SP_X1 - 0.01, SP_TOP)]).close()
           .extrude(GUS_T / 2, both=True)
           .translate((0, gy, 0)))
    body = body.union(gus)

# tab on the -X wall and block in the front-left corner
tab = (box(-XI - 0.01, TAB_X1, TAB_Y[0], TAB_Y[1], F - 0.01, SP_TOP)
       .edges("|Z and >X").fillet(0.4))
body = body.union(tab)
cblk = (box(-XI - 0.01, TAB_X1, -YI - 0.01, CB_Y, F - 0.01, SP_TOP)
        .edges("|Z and >X and >Y").fillet(0.5))
body = body.union(cblk)

# connector cradle in the front-right corner:
#   back strip (with fixing hole and rounded front edge), thin -X side rim,
#   front rim with a channel leading to the front port
strip = box(CR_X0, XI + 0.01, CR_STRIP_Y0, CR_Y1, F - 0.01, CR_TOP)
# ledge in front of the back strip (supports the board's back edge)
strip = strip.cut(box(CR_X0 + CR_RIM, XI + 1, CR_STRIP_Y0 - 1, CR_LEDGE_Y1,
                      CR_LEDGE_Z, CR_TOP + 1))
side_rim = box(CR_X0, CR_X0 + CR_RIM, CR_Y0 - 0.01, CR_STRIP_Y0 + 0.01,
               F - 0.01, CR_BASE_Z)
front_rim = box(CR_X0, XI + 0.01, CR_Y0 - 0.01, CR_POCKET_Y0,
                F - 0.01, CR_BASE_Z)
cradle = strip.union(side_rim).union(front_rim)
cradle = cradle.cut(cq.Workplane("XY").circle(CR_HOLE[2] / 2).extrude(20)
                    .translate((CR_HOLE[0], CR_HOLE[1], F)))
body = body.union(cradle)

# ---------------- lid groove + lowered back wall ----------------
gx = XI + G_DEPTH
gy_ = YI + G_DEPTH
body = body.cut(box(-gx, gx, -gy_, D / 2 + 1, G_FLOOR, G_CEIL))
body = body.cut(box(-XI, XI, YI - 0.01, D / 2 + 1, G_FLOOR, H + 1))

# ---------------- wall openings ----------------
# front port through the -Y wall; the same cutter continues through the
# cradle's front rim to form the connector channel (rounded bottom corners)
fp = box(FP_X0, FP_X1, -D / 2 - 1, CR_POCKET_Y0 + 1.5, FP_Z0, FP_Z1)
fp = fp.edges("|Y and <Z").fillet(FP_R_BOT)
fp = fp.edges("|Y and >Z").fillet(FP_R_TOP)
body = body.cut(fp)

# right side obround slot (through the +X wall)
ss = (cq.Workplane("YZ").center(SS_Y, SS_Z)
      .slot2D(SS_L, SS_H, 0).extrude(T + 2)
      .translate((W / 2 - T - 1, 0, 0)))
body = body.cut(ss)

# left side port (through the -X wall)
lp = (cq.Workplane("YZ").center(LP_Y, LP_Z)
      .rect(LP_W, LP_H).extrude(T + 1.5)
      .translate((-W / 2 - 1, 0, 0)))
lp = lp.edges("|X").fillet(LP_R)
body = body.cut(lp)

# blind round recess on the inner face of the -X wall
lr = (cq.Workplane("YZ").center(LR_Y, LR_Z)
      .circle(LR_D / 2).extrude(LR_DEPTH + 0.5)
      .translate((-XI - LR_DEPTH, 0, 0)))
body = body.cut(lr)

# keyholes through the floor (single closed profile: big circle + slot)
def keyhole(cx, cy):
    w = KH_SLOT_W / 2
    yj = math.sqrt(KH_R ** 2 - w ** 2)          # slot / circle junction
    prof = (cq.Workplane("XY").workplane(offset=-1)
            .moveTo(cx + w, cy + yj)
            .lineTo(cx + w, cy + KH_SLOT_L)
            .threePointArc((cx, cy + KH_SLOT_L + w), (cx - w, cy + KH_SLOT_L))
            .lineTo(cx - w, cy + yj)
            .threePointArc((cx, cy - KH_R), (cx + w, cy + yj))
            .close())
    return prof.extrude(F + 2)


for sx in (-1, 1):
    body = body.cut(keyhole(sx * KH_X, KH_Y))

result = body
